import cadquery as cq

# =====================================================================
#  Cover plate with a recessed plug underneath: four corner countersunk
#  screw holes in shallow square pads, four counterbored square holes
#  and a rectangular window with undercut edges and two small pins.
# =====================================================================

# ---------------- driving dimensions (mm) ----------------
L = 200.0          # plate length (X)
W = 180.0          # plate width (Y)
T = 3.0            # flange (top plate) thickness, top face at z = T
EDGE_R = 1.0       # rounding of the flange outer edges (top, bottom, corners)

BODY_INSET = 10.0  # lower plug inset from flange edge
BODY_H = 4.4       # plug height below flange
RIM_W = 3.5        # plug rim wall width
POCKET_D = 3.3     # depth of pocket cut up into plug from below
CORNER_BOSS = 26.0 # corner boss extent (from plate edge) around screws

# corner screw holes
HOLE_INSET = 18.0
PAD = 16.0         # square pad (shallow recess) around each screw
PAD_D = 0.1
CSK_D = 8.0
HOLE_D = 3.4

# counterbored square holes  (x, y, counterbore diameter)
CB_DEPTH = 3.1
SQ = 9.6
CBORES = [(0.0, 24.3, 19.6), (23.6, 24.3, 19.6), (44.8, 13.7, 19.6), (57.0, -28.1, 25.0)]

# rectangular window: vertical walls at +/-X, undercut (sloped) walls at +/-Y that open
# into a shallow recess in the pocket ceiling; two small locating pins under the overhangs
WIN_C = (56.1, 56.0)
WIN = (25.6, 13.7)
WIN_REC_M = (1.5, 1.5, 5.0, 7.2)      # recess margins around window (-x, +x, -y, +y)
WIN_LIP = 0.4                         # lip thickness left at the +/-Y window edges
PIN_D = 1.8
PIN_L = 3.5
PIN_DX = 8.5                          # pins offset from window centre in X (point symmetric)
PIN_DY = 2.0                          # pins offset outside the window +/-Y edge

# ---------------- flange ----------------
flange = cq.Workplane("XY").box(L, W, T, centered=(True, True, False))
flange = flange.edges("|Z").fillet(EDGE_R)
flange = flange.faces(">Z").edges().fillet(EDGE_R)
flange = flange.faces("<Z").edges().fillet(EDGE_R)

# ---------------- plug (lower body) ----------------
bl, bw = L - 2 * BODY_INSET, W - 2 * BODY_INSET
plug = cq.Workplane("XY").workplane(offset=-BODY_H).rect(bl, bw).extrude(BODY_H)

# pocket from below: inner rectangle minus the four corner screw bosses
pl, pw = bl - 2 * RIM_W, bw - 2 * RIM_W
pocket = cq.Workplane("XY").workplane(offset=-BODY_H).rect(pl, pw).extrude(POCKET_D)
cb = CORNER_BOSS - BODY_INSET
for sx in (-1, 1):
    for sy in (-1, 1):
        cx = sx * (L / 2 - BODY_INSET - cb / 2)
        cy = sy * (W / 2 - BODY_INSET - cb / 2)
        boss = (cq.Workplane("XY").workplane(offset=-BODY_H)
                .center(cx, cy).rect(cb, cb).extrude(POCKET_D))
        pocket = pocket.cut(boss)
plug = plug.cut(pocket)

part = flange.union(plug)

# ---------------- corner screw holes ----------------
hx, hy = L / 2 - HOLE_INSET, W / 2 - HOLE_INSET
corner_pts = [(sx * hx, sy * hy) for sx in (-1, 1) for sy in (-1, 1)]
pads = (cq.Workplane("XY").workplane(offset=T - PAD_D)
        .pushPoints(corner_pts).rect(PAD, PAD).extrude(PAD_D + 1))
part = part.cut(pads)
part = (part.faces(">Z").workplane(origin=(0, 0, T - PAD_D))
        .pushPoints(corner_pts).cskHole(HOLE_D, CSK_D, 90))

# ---------------- counterbored square holes ----------------
for (x, y, d) in CBORES:
    cbore = (cq.Workplane("XY").workplane(offset=T - CB_DEPTH)
             .center(x, y).circle(d / 2).extrude(CB_DEPTH + 1))
    sq = (cq.Workplane("XY").workplane(offset=-BODY_H - 1)
          .center(x, y).rect(SQ, SQ).extrude(BODY_H + T + 2))
    part = part.cut(cbore).cut(sq)

# ---------------- rectangular window ----------------
wx0, wx1 = WIN_C[0] - WIN[0] / 2, WIN_C[0] + WIN[0] / 2
wy0, wy1 = WIN_C[1] - WIN[1] / 2, WIN_C[1] + WIN[1] / 2
rx0, rx1 = wx0 - WIN_REC_M[0], wx1 + WIN_REC_M[1]
ry0, ry1 = wy0 - WIN_REC_M[2], wy1 + WIN_REC_M[3]
# straight through-cut of the window outline
win = (cq.Workplane("XY").workplane(offset=-BODY_H - 1)
       .center(*WIN_C).rect(*WIN).extrude(BODY_H + T + 2))
# recess in the pocket ceiling under the window, up to the flange underside
rec = (cq.Workplane("XY").workplane(offset=-BODY_H - 1)
       .center((rx0 + rx1) / 2, (ry0 + ry1) / 2).rect(rx1 - rx0, ry1 - ry0)
       .extrude(BODY_H + 1))
# undercut: trapezoid (YZ section) from the window lip out to the recess edges
zl = T - WIN_LIP
under = (cq.Workplane("YZ", origin=(wx0, 0, 0))
         .polyline([(ry0, -0.01), (wy0, zl), (wy1, zl), (ry1, -0.01)]).close()
         .extrude(wx1 - wx0))
part = part.cut(win).cut(rec).cut(under)

# two small locating pins hanging from the sloped overhangs
for (px, py, dy) in [(WIN_C[0] - PIN_DX, wy1 + PIN_DY, PIN_DY),
                     (WIN_C[0] + PIN_DX, wy0 - PIN_DY, PIN_DY)]:
    zt = zl * (1 - dy / (WIN_REC_M[3] if py > WIN_C[1] else WIN_REC_M[2]))
    pin = (cq.Workplane("XY").workplane(offset=zt - PIN_L)
           .center(px, py).circle(PIN_D / 2).extrude(PIN_L + 0.3))
    part = part.union(pin)

result = part
